import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Square body (block) with the round front part on the -Y side.
# The axis of all round features runs along Y.
BLOCK_W = 30.0          # X and Z size of square block
BLOCK_D = 10.7          # depth of block along Y (y = 0 .. BLOCK_D)
BULGE_R = 15.5          # through-cylinder slightly proud of block top/bottom
BULGE_FILLET = 12.0     # smooth blend of the bulge into block top/bottom

BACK_DISC_R = 14.9      # round boss on the back face
BACK_DISC_T = 1.12

# mounting ears (left and right, full block depth)
EAR_HOLE_X = 19.55      # hole centre distance from axis
EAR_R = 4.23            # ear end radius (ear height = 2*EAR_R)
EAR_HOLE_D = 4.2

# revolved front part (stacked along -Y from the block front face)
COLLAR_R = 15.0         # large collar in front of block
COLLAR_L = 6.57
NECK_R = 12.65
NECK_L = 7.42
FLANGE_R = 17.1
FLANGE_T = 2.09
CAP_R = 15.07
CAP_L = 4.95
CAP_FLAT_R = 9.5        # flat centre of the push cap face
CAP_ROUND_L = 2.0       # axial depth of the rounded cap rim
CAP_ELL_R0 = 7.5        # radial centre of the elliptic rim profile

FLANGE_FILLET = 0.5
COLLAR_FILLET = 0.4
JOINT_FILLET = 0.35

# ---------------- derived positions ----------------
y_collar = -COLLAR_L
y_neck = y_collar - NECK_L
y_flange = y_neck - FLANGE_T
y_cap = y_flange - CAP_L

# ---------------- revolved front part ----------------
# elliptic rim of the cap: centre (CAP_ELL_R0, y_cap + CAP_ROUND_L), ends tangent
# to the cap cylinder and starts at the edge of the flat face
_ell_a = CAP_R - CAP_ELL_R0
_u = (CAP_FLAT_R - CAP_ELL_R0) / _ell_a
_ell_b = CAP_ROUND_L / math.sqrt(1.0 - _u * _u)
_ell_t0 = 360.0 - math.degrees(math.acos(_u))
# profile drawn in the XY plane: x = radius, y = axial position
prof = (
    cq.Workplane("XY")
    .moveTo(0, y_cap)
    .lineTo(CAP_FLAT_R, y_cap)
    .ellipseArc(_ell_a, _ell_b, angle1=_ell_t0, angle2=360, sense=1,
                startAtCurrent=True)
    .lineTo(CAP_R, y_flange)
    .lineTo(FLANGE_R, y_flange)
    .lineTo(FLANGE_R, y_neck)
    .lineTo(NECK_R, y_neck)
    .lineTo(NECK_R, y_collar)
    .lineTo(COLLAR_R, y_collar)
    .lineTo(COLLAR_R, 0.0)
    .lineTo(0, 0.0)
    .close()
)
front = prof.revolve(360, (0, 0, 0), (0, 1, 0))


def _circ_edges(shape, radius, y, tol=0.05):
    """circular edges of given radius lying in the plane y = const"""
    out = []
    for e in shape.Edges():
        if e.geomType() != "CIRCLE":
            continue
        bb = e.BoundingBox()
        if abs(bb.ymin - y) < tol and abs(bb.ymax - y) < tol and abs(e.radius() - radius) < tol:
            out.append(e)
    return out


fs = front.val()
# round both rims of the thin flange
fs = fs.fillet(FLANGE_FILLET, _circ_edges(fs, FLANGE_R, y_flange) + _circ_edges(fs, FLANGE_R, y_neck))
# small blends where flange meets cap and neck
fs = fs.fillet(JOINT_FILLET, _circ_edges(fs, CAP_R, y_flange) + _circ_edges(fs, NECK_R, y_neck))
# rounded front rim of the collar
fs = fs.fillet(COLLAR_FILLET, _circ_edges(fs, COLLAR_R, y_collar))
# turn the revolve seam to the underside (-Z), where the original has its seam
fs = fs.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)
front = cq.Workplane("XY").add(fs)

# ---------------- square block with shallow bulge ----------------
# Workplane "XZ" has its normal along -Y, so a negative extrude grows toward +Y
block = cq.Workplane("XZ").rect(BLOCK_W, BLOCK_W).extrude(-BLOCK_D)
bulge = cq.Workplane("XZ").circle(BULGE_R).extrude(-BLOCK_D)
core = block.union(bulge)


def _bulge_edge(e):
    bb = e.BoundingBox()
    return ((bb.ymax - bb.ymin) > 1.0 and abs(bb.xmin) < BLOCK_W / 3
            and abs(abs(bb.zmin) - BLOCK_W / 2) < 0.01)


core = cq.Workplane("XY").add(
    core.val().fillet(BULGE_FILLET, [e for e in core.edges().vals() if _bulge_edge(e)])
)

back_disc = (
    cq.Workplane("XZ", origin=(0, BLOCK_D, 0))
    .circle(BACK_DISC_R)
    .extrude(-BACK_DISC_T)
)

# ---------------- mounting ears ----------------
ears = (
    cq.Workplane("XZ")
    .slot2D(2 * EAR_HOLE_X + 2 * EAR_R, 2 * EAR_R)
    .extrude(-BLOCK_D)
)
holes = (
    cq.Workplane("XZ", origin=(0, -1.0, 0))
    .pushPoints([(-EAR_HOLE_X, 0), (EAR_HOLE_X, 0)])
    .circle(EAR_HOLE_D / 2)
    .extrude(-(BLOCK_D + 2.0))
)

body = core.union(back_disc).union(ears).cut(holes)

result = front.union(body)

VIEW = {"azimuth": 45, "elevation": 26}
